import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
W = 80.0            # square base plate side
T = 8.9             # base plate thickness
RC = 4.5            # plate vertical corner radius
R_EDGE = 0.9        # plate top outer edge round

H = 91.3            # overall height
RB = 38.0           # body radius at plate top
RS = 36.1           # body radius at shoulder corner
ZS = 77.8           # shoulder corner height
RN = 30.6           # neck (top cap) radius
ZN = 84.6           # neck start height
F_SH = 9.0          # convex shoulder round
F_NK = 1.5          # concave fillet at neck
F_BASE = 3.0        # body-to-plate fillet
SEAM_ANGLE = 90.0   # where the revolve seam sits (cosmetic)

HOLE_P = 32.5       # corner hole position (+/-)
HOLE_D = 5.6        # corner hole diameter
HOLE_CH = 0.4       # corner hole top chamfer
SPOT_IN = 6.0       # spot face extent toward the body side (from hole axis)
SPOT_RIN = 5.0      # spot face inner corner radius
SPOT_RS = 1.5       # spot face side corner radius
SPOT_DEPTH = 0.8    # spot face depth
PIN_D = 2.8         # locating pin hole diameter
PIN_OFF = (-5.7, 2.6)   # pin offset from the (+,+) corner hole (point symmetric copy)

# bottom recess
POCK_HALF = 38.4    # octagon flats (parallel to plate edges)
POCK_DIAG = 54.0    # octagon chamfer flats: |x|+|y| = POCK_DIAG
POCK_DEPTH = 1.0
POCK_BULGE = 0.8    # outward bulge of the corner chords
NOTCH_R = 1.2
DISK_R = 27.0
DISK_DEPTH = 0.5

# +X side boss
BOSS_W = 20.0
BOSS_XIN = 28.0     # inner end of both side bosses (buried in the body)
BOSS_XR = 41.8      # outer face x
BOSS_HR = 21.2      # top height
BOSS_R = 1.5        # top edge round
BOSS_RV = 2.0       # outer vertical edge round
PAD_W = 17.1
PAD_H = 16.3
PAD_ZC = 11.3
PAD_T = 1.0
PAD_TL = 0.5
PAD_HOLE_D = 4.7
PAD_HOLE_DEPTH = 0.35

# -X side boss with cable connector elbow
BOSS_XL = -42.5
BOSS_HL = 19.4
PORT_Z = 10.3        # connector axis height
PORT_R = 6.1        # connector tube radius
FL_S = 12.0         # connector flange square
FL_T = 2.4          # connector flange thickness
SCREW_R = 1.4
SCREW_H = 1.0
SCREW_PITCH = 9.2
PORT_XEND = -60.6   # outer extent of elbow in -X
PORT_YEND = -24.2   # end of elbow leg in -Y

# ---------------------------------------------------------------- base plate + body
footprint = cq.Workplane("XY").rect(W, W).extrude(H).edges("|Z").fillet(RC)
plate = cq.Workplane("XY").rect(W, W).extrude(T).edges("|Z").fillet(RC)

# revolved body; the concave base fillet is part of the profile so it can run
# past the plate edge at the mid-sides, where it is trimmed by the footprint
c45 = math.sqrt(0.5)
body = (
    cq.Workplane("XZ")
    .moveTo(0.0, T)
    .lineTo(RB + F_BASE, T)
    .threePointArc(
        (RB + F_BASE - c45 * F_BASE, T + F_BASE - c45 * F_BASE),
        (RB, T + F_BASE),
    )
    .lineTo(RS, ZS)
    .lineTo(RN, ZN)
    .lineTo(RN, H)
    .lineTo(0.0, H)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.edges(cq.selectors.BoxSelector((-50, -50, ZS - 0.01), (50, 50, ZS + 0.01))).fillet(F_SH)
body = body.edges(cq.selectors.BoxSelector((-50, -50, ZN - 0.01), (50, 50, ZN + 0.01))).fillet(F_NK)
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
body = body.intersect(footprint)

part = plate.union(body)


class _OuterTopEdges(cq.Selector):
    """edges of the plate's top outer perimeter"""

    def filter(self, objs):
        out = []
        lim = W / 2 - 0.3 * RC
        for e in objs:
            bb = e.BoundingBox()
            if bb.zmin < T - 0.01 or bb.zmax > T + 1.0:
                continue
            c = e.Center()
            if max(abs(c.x), abs(c.y)) > lim:
                out.append(e)
        return out


part = part.edges(_OuterTopEdges()).fillet(R_EDGE)

# ---------------------------------------------------------------- +X boss
boss_r = (
    cq.Workplane("XY")
    .box(BOSS_XR - BOSS_XIN, BOSS_W, BOSS_HR, centered=(False, True, False))
    .translate((BOSS_XIN, 0, 0))
    .edges("|Z and >X")
    .fillet(BOSS_RV)
    .faces(">Z")
    .edges()
    .fillet(BOSS_R)
)
pad_r = (
    cq.Workplane("YZ", origin=(BOSS_XR, 0, 0))
    .center(0, PAD_ZC)
    .rect(PAD_W, PAD_H)
    .extrude(PAD_T)
    .edges("|X")
    .fillet(1.5)
)
part = part.union(boss_r).union(pad_r)
part = part.cut(
    cq.Workplane("YZ", origin=(BOSS_XR + PAD_T, 0, 0))
    .center(0, PAD_ZC)
    .circle(PAD_HOLE_D / 2)
    .extrude(-PAD_HOLE_DEPTH)
)

# ---------------------------------------------------------------- -X boss + connector elbow
boss_l = (
    cq.Workplane("XY")
    .box(-BOSS_XL - BOSS_XIN, BOSS_W, BOSS_HL, centered=(False, True, False))
    .translate((BOSS_XL, 0, 0))
    .edges("|Z and <X")
    .fillet(BOSS_RV)
    .faces(">Z")
    .edges()
    .fillet(BOSS_R)
)
pad_l = (
    cq.Workplane("YZ", origin=(BOSS_XL, 0, 0))
    .center(0, PORT_Z)
    .rect(PAD_W - 1.0, PAD_H - 2.0)
    .extrude(-PAD_TL)
    .edges("|X")
    .fillet(1.5)
)
x_fl0 = BOSS_XL - PAD_TL
flange = (
    cq.Workplane("YZ", origin=(x_fl0, 0, 0))
    .center(0, PORT_Z)
    .rect(FL_S, FL_S)
    .extrude(-FL_T)
    .edges("|X")
    .fillet(1.0)
)
screws = (
    cq.Workplane("YZ", origin=(x_fl0 - FL_T, 0, 0))
    .center(0, PORT_Z)
    .rect(SCREW_PITCH, SCREW_PITCH, forConstruction=True)
    .vertices()
    .circle(SCREW_R)
    .extrude(-SCREW_H)
)
x_tube0 = x_fl0 - FL_T
xb = PORT_XEND + PORT_R            # elbow leg axis x
tube_a = (
    cq.Workplane("YZ", origin=(x_tube0, 0, 0))
    .center(0, PORT_Z)
    .circle(PORT_R)
    .extrude(PORT_XEND - x_tube0)
)
tube_b = (
    cq.Workplane("XZ")
    .center(xb, PORT_Z)
    .circle(PORT_R)
    .extrude(-PORT_YEND)            # XZ normal is -Y
)
part = (
    part.union(boss_l)
    .union(pad_l)
    .union(flange)
    .union(screws)
    .union(tube_a)
    .union(tube_b)
)

# ---------------------------------------------------------------- corner spot faces, holes, pins
def spot_outline(sx, sy):
    """closed outline of one corner spot face (hole at (sx*P, sy*P))"""
    hx, hy = sx * HOLE_P, sy * HOLE_P
    so = W / 2 - HOLE_P - R_EDGE          # reaches the start of the edge round
    ro = RC - R_EDGE                      # concentric with the plate corner
    si, ri, rs = SPOT_IN, SPOT_RIN, SPOT_RS

    def P(u, v):                          # local (+,+) frame -> world
        return (hx + sx * u, hy + sy * v)

    k = 1.0 - c45
    w = (
        cq.Workplane("XY", origin=(0, 0, T - SPOT_DEPTH))
        .moveTo(*P(-si, -si + ri))
        .lineTo(*P(-si, so - rs))
        .threePointArc(P(-si + rs * k, so - rs * k), P(-si + rs, so))
        .lineTo(*P(so - ro, so))
        .threePointArc(P(so - ro * k, so - ro * k), P(so, so - ro))
        .lineTo(*P(so, -si + rs))
        .threePointArc(P(so - rs * k, -si + rs * k), P(so - rs, -si))
        .lineTo(*P(-si + ri, -si))
        .threePointArc(P(-si + ri * k, -si + ri * k), P(-si, -si + ri))
        .close()
    )
    return w.extrude(SPOT_DEPTH + 3.0)


spot = None
for sx in (-1, 1):
    for sy in (-1, 1):
        s = spot_outline(sx, sy)
        spot = s if spot is None else spot.union(s)
part = part.cut(spot)

pts = [(sx * HOLE_P, sy * HOLE_P) for sx in (-1, 1) for sy in (-1, 1)]
holes = cq.Workplane("XY", origin=(0, 0, -1)).pushPoints(pts).circle(HOLE_D / 2).extrude(T + 2)
part = part.cut(holes)
for p in pts:
    cone = cq.Solid.makeCone(
        HOLE_D / 2, HOLE_D / 2 + HOLE_CH + 0.3,
        HOLE_CH + 0.3,
        cq.Vector(p[0], p[1], T - SPOT_DEPTH - HOLE_CH),
        cq.Vector(0, 0, 1),
    )
    part = part.cut(cq.Workplane().add(cone))

pin_pts = [
    (HOLE_P + PIN_OFF[0], HOLE_P + PIN_OFF[1]),
    (-HOLE_P - PIN_OFF[0], -HOLE_P - PIN_OFF[1]),
]
pins = cq.Workplane("XY", origin=(0, 0, -1)).pushPoints(pin_pts).circle(PIN_D / 2).extrude(T + 2)
part = part.cut(pins)

# ---------------------------------------------------------------- bottom recess
v = POCK_DIAG - POCK_HALF
_m = POCK_DIAG / 2 + POCK_BULGE * c45          # bulged chord mid-point (per axis)
oct_p = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .moveTo(POCK_HALF, -v)
    .lineTo(POCK_HALF, v)
    .threePointArc((_m, _m), (v, POCK_HALF))
    .lineTo(-v, POCK_HALF)
    .threePointArc((-_m, _m), (-POCK_HALF, v))
    .lineTo(-POCK_HALF, -v)
    .threePointArc((-_m, -_m), (-v, -POCK_HALF))
    .lineTo(v, -POCK_HALF)
    .threePointArc((_m, -_m), (POCK_HALF, -v))
    .close()
    .extrude(1 + POCK_DEPTH)
)
notch_pts = []
for a, b in ((POCK_HALF, v), (v, POCK_HALF)):
    for sx in (-1, 1):
        for sy in (-1, 1):
            notch_pts.append((sx * a, sy * b))
notches = cq.Workplane("XY", origin=(0, 0, -1)).pushPoints(notch_pts).circle(NOTCH_R).extrude(1 + POCK_DEPTH)
part = part.cut(oct_p.union(notches))
disk = cq.Workplane("XY", origin=(0, 0, -1)).circle(DISK_R).extrude(1 + POCK_DEPTH + DISK_DEPTH)
part = part.cut(disk)

result = part
